import math
import cadquery as cq

# ---- driving dimensions (mm) ----
L = 100.0          # block length (X)
W = 76.4           # block width (Y)
T = 16.0           # block thickness (Z)

DISH_A = 69.3      # dish rim length (X)
DISH_B = 54.0      # dish rim width (Y)
DISH_D = 8.5       # dish depth
DISH_R = 6.0       # radius of the rounded dish floor edge (wall above is straight)
DISH_X = 1.1       # dish centre offset in X

HOLE_D = 6.1       # drain hole diameter at the dish floor
HOLE_D_BOT = 13.0  # drain hole diameter at the underside (tapered hole)
HOLE_X = -1.7      # drain hole offset in X

HEX_AF = 10.1      # hex pocket across flats at the top face
HEX_AF_BOT = 8.6   # hex pocket across flats at its floor (drafted walls)
HEX_DEPTH = 2.4    # hex pocket depth
HEX_XL = 10.2      # hex centre distance from the -X edge
HEX_XR = 10.8      # hex centre distance from the +X edge
HEX_Y = 9.5        # hex centre distance from the Y edges
HEX_ROT = 4.0      # small rotation of hex pockets (deg)

VIEW = {"azimuth": 45, "elevation": 26}

# base block, bottom at z=0
block = cq.Workplane("XY").box(L, W, T, centered=(True, True, False))

# elliptical dish: straight wall, rounded floor edge, flat floor
dish_tool = (
    cq.Workplane("XY")
    .workplane(offset=T - DISH_D)
    .center(DISH_X, 0)
    .ellipse(DISH_A / 2.0, DISH_B / 2.0)
    .extrude(DISH_D + 2.0)
    .faces("<Z")
    .edges()
    .fillet(DISH_R)
)
body = block.cut(dish_tool)

# tapered drain hole: wide on the underside, narrow at the dish floor
floor_z = T - DISH_D
hole_tool = cq.Solid.makeCone(
    HOLE_D_BOT / 2.0,
    HOLE_D / 2.0,
    floor_z,
    cq.Vector(HOLE_X, 0, 0),
    cq.Vector(0, 0, 1),
)
# extend the small end straight up through the floor so the cut is clean
hole_top = cq.Solid.makeCylinder(
    HOLE_D / 2.0, DISH_D, cq.Vector(HOLE_X, 0, floor_z), cq.Vector(0, 0, 1)
)
body = body.cut(cq.Workplane("XY").add(hole_tool)).cut(cq.Workplane("XY").add(hole_top))

# drafted hex pockets at the four corners (vertex pointing along Y)
k = 1.0 / math.cos(math.radians(30))          # across-flats -> across-corners
hex_taper = math.degrees(math.atan((HEX_AF - HEX_AF_BOT) / 2.0 / HEX_DEPTH))
pts = [
    (-L / 2.0 + HEX_XL, -W / 2.0 + HEX_Y),
    (-L / 2.0 + HEX_XL, W / 2.0 - HEX_Y),
    (L / 2.0 - HEX_XR, -W / 2.0 + HEX_Y),
    (L / 2.0 - HEX_XR, W / 2.0 - HEX_Y),
]
for (px, py) in pts:
    tool = (
        cq.Workplane("XY")
        .workplane(offset=T)
        .polygon(6, HEX_AF * k)
        .extrude(-HEX_DEPTH, taper=hex_taper)
        .rotate((0, 0, 0), (0, 0, 1), 90 + HEX_ROT)
        .translate((px, py, 0))
    )
    body = body.cut(tool)

result = body
